import cadquery as cq
import math

# =====================================================================
#  Electronics control-unit housing with a screwed front connector plate
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 200.0          # body width (X)
L_TOT = 199.0      # plate front face to back face (Y)
T_PLATE = 13.0     # front cover plate depth (Y)
H_FRONT = 67.2     # height of cover plate and raised front strip
H_MAIN = 56.4      # body height over the main (rear) top
STRIP_LEN = 27.0   # flat raised strip length behind the plate
COVE_LEN = 35.5    # length of the concave transition down to the main top
CREST_R = 4.0      # convex round at the top of the cove
WALL = 3.0         # shell wall thickness
FRONT_WALL = 3.5   # cover plate front wall thickness
PLATE_FILLET = 3.0 # rounded front perimeter of the cover plate
OPEN_FILLET = 1.2  # rounded lips of the connector openings
RHOLE_FILLET = 0.6 # rounded lip of the round hole

TAB_T = 4.5        # mounting tab thickness
TAB_W = 34.0       # tab width along Y at the body
TAB_OUT = 14.5     # tab protrusion from the side wall
TAB_HOLE_D = 6.8
TAB_HOLE_IN = 7.3  # hole centre distance from side wall
TAB_BLEND = 3.0   # concave blend radius ear / wall
TAB_Y = (42.5, 166.5)   # tab centres measured from the plate front

BOSS_R = 4.1       # corner screw boss radius
BOSS_IN_X = 3.6    # boss centre inset from the plate sides
BOSS_IN_Z = 3.0    # boss centre inset from plate top / bottom
MID_BOSS_R = 4.2   # top-middle screw boss (runs back over the strip)
MID_BOSS_LIFT = 0.4
MID_BOSS_LEN = 15.0
MID_BOSS_FILLET = 1.5
MID_BOSS_END_C = 2.0  # bevelled rear end of the top boss
HEX_D = 5.0        # hex socket across corners
HEX_DEPTH = 2.5

# front connector openings
OPEN_W, OPEN_H, OPEN_R = 44.6, 29.0, 3.0     # connector cut-out core
EAR_W, EAR_H, EAR_R = 52.0, 14.0, 2.0        # side ears of the cut-out
OPEN_Z = 38.6
OPEN_X = (-52.5, 22.6)
RHOLE_X, RHOLE_Z, RHOLE_D = 74.4, 48.6, 25.0  # round connector hole

# rear panel holes: (x, z) centres and sizes
REAR_ROUND = (74.4, 37.5, 10.0)                  # x, z, diameter
REAR_SLOTS = [(35.0, 34.0), (10.0, 34.0)]        # slot centres
REAR_SLOT_L, REAR_SLOT_W = 12.5, 6.3
REAR_RECT1 = (-26.3, 22.5, 21.0, 13.0, 3.0)      # x, z, w, h, corner r
REAR_RECT2 = (-62.2, 26.5, 23.5, 19.0, 1.0)

# card-guide rails inside
RAIL_Z = (13.5, 19.0)
RAIL_T, RAIL_D = 2.0, 3.5

VIEW = {"azimuth": 45, "elevation": 26}

y_front = -L_TOT / 2.0
y_body = y_front + T_PLATE       # body front face (behind plate)
y_back = L_TOT / 2.0
y_strip_end = y_body + STRIP_LEN
y_cove_end = y_strip_end + COVE_LEN
DROP = H_FRONT - H_MAIN

# normalised cove profile (fraction of length, fraction of drop)
COVE_PTS = [(0.0, 0.0), (0.268, 0.388), (0.511, 0.724), (0.754, 0.922), (1.0, 1.0)]

# ---------------- body (side profile extruded across X) ----------------
cove = [(y_strip_end + u * COVE_LEN, H_FRONT - v * DROP) for (u, v) in COVE_PTS]
body = (
    cq.Workplane("YZ", origin=(-W / 2, 0, 0))
    .moveTo(y_body, 0)
    .lineTo(y_back, 0)
    .lineTo(y_back, H_MAIN)
    .lineTo(cove[-1][0], cove[-1][1])
    .spline(list(reversed(cove))[1:], tangents=[(-1, 0), (-1, 0.55)], includeCurrent=True)
    .lineTo(y_body, H_FRONT)
    .close()
    .extrude(W)
)
# soften the crest where the raised strip rolls over into the cove
body = body.edges(
    cq.selectors.BoxSelector((-W, y_strip_end - 0.2, H_FRONT - 0.2), (W, y_strip_end + 0.2, H_FRONT + 0.2))
).fillet(CREST_R)
# hollow it, leaving the front open (closed by the cover plate)
body = body.faces("<Y").shell(-WALL)

# card-guide rails on the inner side walls
for side in (-1, 1):
    for rz in RAIL_Z:
        rail = (
            cq.Workplane("XY")
            .box(RAIL_D + 0.5, y_back - WALL - y_body, RAIL_T, centered=(True, False, True))
            .translate((side * (W / 2 - WALL - RAIL_D / 2 + 0.25), y_body, rz))
        )
        body = body.union(rail)

# ---------------- front cover plate (cap) ----------------
plate = (
    cq.Workplane("XY")
    .box(W, T_PLATE, H_FRONT, centered=(True, False, False))
    .translate((0, y_front, 0))
)
plate = plate.faces("<Y").edges().fillet(PLATE_FILLET)
# pocket behind the front wall, matching the body cavity
plate = plate.cut(
    cq.Workplane("XY")
    .box(W - 2 * WALL, T_PLATE - FRONT_WALL, H_FRONT - 2 * WALL, centered=(True, False, False))
    .translate((0, y_front + FRONT_WALL, WALL))
)

result = body.union(plate)

# ---------------- front openings ----------------
def front_sketch(x, z):
    return cq.Workplane("XZ", origin=(0, y_front - 1, 0)).center(x, z)


def connector_cut(x):
    core = (
        front_sketch(x, OPEN_Z).rect(OPEN_W, OPEN_H)
        .extrude(-(FRONT_WALL + 2)).edges("|Y").fillet(OPEN_R)
    )
    ear = (
        front_sketch(x, OPEN_Z).rect(EAR_W, EAR_H)
        .extrude(-(FRONT_WALL + 2)).edges("|Y").fillet(EAR_R)
    )
    return core.union(ear)


cuts = connector_cut(OPEN_X[0]).union(connector_cut(OPEN_X[1]))
cuts = cuts.union(front_sketch(RHOLE_X, RHOLE_Z).circle(RHOLE_D / 2).extrude(-(FRONT_WALL + 2)))
# small key notch of the round hole
cuts = cuts.union(front_sketch(RHOLE_X - RHOLE_D / 2, RHOLE_Z).rect(3.0, 2.0).extrude(-(FRONT_WALL + 2)))
result = result.cut(cuts)

# soften the outer lips of the openings
for (x0, x1, z0, z1) in [
    (OPEN_X[0] - EAR_W / 2 - 1, OPEN_X[0] + EAR_W / 2 + 1, OPEN_Z - OPEN_H / 2 - 1, OPEN_Z + OPEN_H / 2 + 1),
    (OPEN_X[1] - EAR_W / 2 - 1, OPEN_X[1] + EAR_W / 2 + 1, OPEN_Z - OPEN_H / 2 - 1, OPEN_Z + OPEN_H / 2 + 1),
]:
    result = result.edges(
        cq.selectors.BoxSelector((x0, y_front - 0.2, z0), (x1, y_front + 0.2, z1))
    ).fillet(OPEN_FILLET)
result = result.edges(
    cq.selectors.BoxSelector((RHOLE_X - RHOLE_D / 2 - 3, y_front - 0.2, RHOLE_Z - RHOLE_D / 2 - 1),
                             (RHOLE_X + RHOLE_D / 2 + 1, y_front + 0.2, RHOLE_Z + RHOLE_D / 2 + 1))
).fillet(RHOLE_FILLET)

# ---------------- screw bosses (axis along Y) ----------------
corner_pts = [
    (-W / 2 + BOSS_IN_X, H_FRONT - BOSS_IN_Z), (W / 2 - BOSS_IN_X, H_FRONT - BOSS_IN_Z),
    (-W / 2 + BOSS_IN_X, BOSS_IN_Z), (W / 2 - BOSS_IN_X, BOSS_IN_Z),
    (0.0, BOSS_IN_Z),
]
bosses = (
    cq.Workplane("XZ", origin=(0, y_body, 0))
    .pushPoints(corner_pts)
    .circle(BOSS_R)
    .extrude(T_PLATE)
    .faces("<Y").edges().fillet(0.8)
)
# top-middle boss: cylinder blended into the top surface by concave flares,
# built as one cross-section (XZ) extruded along Y
_R, _rf, _lift = MID_BOSS_R, MID_BOSS_FILLET, MID_BOSS_LIFT
_cz = H_FRONT + _lift
_xc = math.sqrt((_R + _rf) ** 2 - (_rf - _lift) ** 2)      # flare centre x
_k = _R / (_R + _rf)
_tx, _tz = _xc * _k, _cz + (H_FRONT + _rf - _cz) * _k       # tangent point on boss circle


def _flare_mid(sx):
    """mid point of the concave flare arc (centre (sx*_xc, H+rf))."""
    ang0 = math.atan2(H_FRONT - (H_FRONT + _rf), 0.0)
    ang1 = math.atan2(_tz - (H_FRONT + _rf), _tx - _xc)
    am = 0.5 * (ang0 + ang1)
    return (sx * (_xc + _rf * math.cos(am)), H_FRONT + _rf + _rf * math.sin(am))


top_boss = (
    cq.Workplane("XZ", origin=(0, y_front + MID_BOSS_LEN, 0))
    .moveTo(-_xc, H_FRONT - 1.0)
    .lineTo(_xc, H_FRONT - 1.0)
    .lineTo(_xc, H_FRONT)
    .threePointArc(_flare_mid(1), (_tx, _tz))
    .threePointArc((0.0, _cz + _R), (-_tx, _tz))
    .threePointArc(_flare_mid(-1), (-_xc, H_FRONT))
    .close()
    .extrude(MID_BOSS_LEN)
    .faces(">Y").edges("%CIRCLE").chamfer(MID_BOSS_END_C)
)
result = result.union(bosses).union(top_boss)

# hex screw sockets in the boss fronts
sockets = (
    cq.Workplane("XZ", origin=(0, y_front, 0))
    .pushPoints(corner_pts)
    .polygon(6, HEX_D)
    .extrude(-HEX_DEPTH)
)
result = result.cut(sockets)
# hex screw socket in the top boss front
result = result.cut(
    cq.Workplane("XZ", origin=(0, y_front, 0))
    .center(0.0, _cz)
    .polygon(6, HEX_D)
    .extrude(-HEX_DEPTH)
)

# ---------------- rear panel holes ----------------
def rear(x, z):
    return cq.Workplane("XZ", origin=(0, y_back + 1, 0)).center(x, z)


rear_cuts = rear(REAR_ROUND[0], REAR_ROUND[1]).circle(REAR_ROUND[2] / 2).extrude(WALL + 2)
for (sx, sz) in REAR_SLOTS:
    rear_cuts = rear_cuts.union(rear(sx, sz).slot2D(REAR_SLOT_L, REAR_SLOT_W).extrude(WALL + 2))
for (rx, rz, rw, rh, rr) in (REAR_RECT1, REAR_RECT2):
    rear_cuts = rear_cuts.union(rear(rx, rz).rect(rw, rh).extrude(WALL + 2).edges("|Y").fillet(rr))
result = result.cut(rear_cuts)

# ---------------- mounting tabs ----------------
def ear_profile(side, yc):
    """teardrop mounting ear on side wall (side=+1/-1) centred at yc."""
    r_tip = TAB_OUT - TAB_HOLE_IN
    d = TAB_HOLE_IN
    h = TAB_W / 2
    # tangent from wall point (0, h) to the tip circle centred (d, 0)
    dist = math.hypot(-d, h)
    base = math.atan2(h, -d)
    off = math.acos(r_tip / dist)
    t_ang = base - off
    tx, ty = d + r_tip * math.cos(t_ang), r_tip * math.sin(t_ang)

    def g(u, v):
        return (side * (W / 2 + u), yc + v)

    wp = (
        cq.Workplane("XY")
        .moveTo(*g(-1.0, -h))
        .lineTo(*g(-1.0, h))
        .lineTo(*g(0.0, h))
        .lineTo(*g(tx, ty))
        .threePointArc(g(d + r_tip, 0), g(tx, -ty))
        .lineTo(*g(0.0, -h))
        .close()
        .extrude(TAB_T)
    )
    hole = cq.Workplane("XY").center(side * (W / 2 + d), yc).circle(TAB_HOLE_D / 2).extrude(TAB_T)
    return wp.cut(hole)


for side in (-1, 1):
    for ty in TAB_Y:
        yc = y_front + ty
        result = result.union(ear_profile(side, yc))
        # concave blends where the ear meets the side wall
        for sv in (-1, 1):
            px, py = side * W / 2, yc + sv * TAB_W / 2
            result = result.edges(
                cq.selectors.BoxSelector((px - 0.3, py - 0.3, 0.5), (px + 0.3, py + 0.3, TAB_T - 0.5))
            ).fillet(TAB_BLEND)
